import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Flat 90-degree elbow cover for a cable raceway.
# A thin C-shaped channel profile (flat top, rounded top corners, slightly
# convex splayed side walls, round retaining beads along the bottom edges)
# carried along an L-shaped path: straight leg (+Y) / quarter bend / straight
# leg (+X).  Built from exact features: extrude + revolve + mirrored extrude.
# ---------------------------------------------------------------------------

# driving dimensions (mm)
W = 60.0          # width of the channel profile (outer, across the beads)
H = 22.0          # overall height (outer top)
T = 2.05          # wall thickness
RB = 3.2          # radius of the bottom retaining beads
RO = 8.15         # outer radius of the top corners of the profile
RW = 85.0         # radius of the (slightly convex) side walls
BETA = 16.0       # side wall lean at the bead (degrees from vertical)
R_IN = 8.4        # inner bend radius (plan view, at the beads)
LEG = 43.1        # straight leg length measured from the bend centre

RC = R_IN + W / 2.0   # bend radius of the profile centre line
XC = -RC              # the +Y leg is centred on X = XC, the +X leg on Y = XC


def pol(c, r, ang):
    return (c[0] + r * math.cos(ang), c[1] + r * math.sin(ang))


def mir(p):
    return (-p[0], p[1])


def profile_points():
    """Key points of the right half (s >= 0) of the profile, in (s, z)."""
    b = math.radians(BETA)
    cb = (W / 2.0 - RB, RB)                              # bead centre
    cw = pol(cb, -(RW - RB), b)                          # side-wall arc centre
    zc = H - RO
    sc = cw[0] + math.sqrt((RW - RO) ** 2 - (zc - cw[1]) ** 2)
    co = (sc, zc)                                        # corner arc centre
    psi = math.atan2(co[1] - cw[1], co[0] - cw[0])       # wall/corner tangency

    # outer contour
    A1 = (sc, H)                                         # end of flat top
    Am = pol(co, RO, (psi + math.pi / 2) / 2)
    A2 = pol(co, RO, psi)                                # corner -> wall
    Wm = pol(cw, RW, (psi + b) / 2)
    Tp = pol(cb, RB, b)                                  # wall -> bead
    # bead / inner wall intersection (small re-entrant notch)
    D = RW - RB
    cphi = ((RW - T) ** 2 - D * D - RB * RB) / (2 * D * RB)
    phi = b + math.acos(cphi)
    Pp = pol(cb, RB, phi)
    Bm = pol(cb, RB, (b + phi - 2 * math.pi) / 2)        # round the bead
    # inner contour (offset of the outer one by T)
    psi_p = math.atan2(Pp[1] - cw[1], Pp[0] - cw[0])
    Im = pol(cw, RW - T, (psi_p + psi) / 2)
    B2 = pol(co, RO - T, psi)
    Bmid = pol(co, RO - T, (psi + math.pi / 2) / 2)
    B1 = (sc, H - T)
    return dict(A1=A1, Am=Am, A2=A2, Wm=Wm, Tp=Tp, Bm=Bm, Pp=Pp, Im=Im,
                B2=B2, Bmid=Bmid, B1=B1)


def profile_segments():
    """Closed profile as a list of ('l', p0, p1) / ('a', p0, pmid, p1)."""
    p = profile_points()
    A1, Am, A2, Wm, Tp = p["A1"], p["Am"], p["A2"], p["Wm"], p["Tp"]
    Bm, Pp, Im, B2, Bmid, B1 = p["Bm"], p["Pp"], p["Im"], p["B2"], p["Bmid"], p["B1"]
    outer = [("a", mir(Pp), mir(Bm), mir(Tp)),        # left bead
             ("a", mir(Tp), mir(Wm), mir(A2)),        # left side wall
             ("a", mir(A2), mir(Am), mir(A1)),        # left top corner
             ("l", mir(A1), A1),                      # flat top
             ("a", A1, Am, A2),                       # right top corner
             ("a", A2, Wm, Tp),                       # right side wall
             ("a", Tp, Bm, Pp)]                       # right bead
    inner = [("a", Pp, Im, B2),                       # right inner wall
             ("a", B2, Bmid, B1),                     # right inner corner
             ("l", B1, mir(B1)),                      # underside of top
             ("a", mir(B1), mir(Bmid), mir(B2)),      # left inner corner
             ("a", mir(B2), mir(Im), mir(Pp))]        # left inner wall
    return outer + inner


def profile(wp):
    segs = profile_segments()
    wp = wp.moveTo(*segs[0][1])
    for sg in segs:
        if sg[0] == "l":
            wp = wp.lineTo(*sg[2])
        else:
            wp = wp.threePointArc(sg[2], sg[3])
    return wp.close()


# profile plane at Y = 0 centred on X = XC: local x = -X, local y = +Z,
# normal = +Y (so the extrusion runs along +Y)
plane = cq.Plane(origin=(XC, 0, 0), xDir=(-1, 0, 0), normal=(0, 1, 0))

# straight leg running along +Y
leg_y = profile(cq.Workplane(plane)).extrude(LEG)

# quarter bend about the vertical axis through the bend centre (origin)
bend = profile(cq.Workplane(plane)).revolve(90.0, (XC, 0, 0), (XC, 1, 0))

# straight leg running along +X: mirror image of the +Y leg about X = Y
leg_x = leg_y.mirror(mirrorPlane=(1, -1, 0), basePointVector=(0, 0, 0))

result = leg_y.union(bend).union(leg_x).clean()

VIEW = {"azimuth": 45, "elevation": 26}
